"""Clamp / mounting block: a flat base plate with a full-width centre boss.

* base plate with two counterbored mounting holes (drill-point counterbore floors)
* centre boss pierced vertically by a rounded-rectangle window (through the base too),
  whose lowest few millimetres are relieved very slightly
* a counterbored cross hole through the boss along Y (set-screw hole into the window)
* 3 mm fillets on every upper edge, small chamfer round the underside
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length (X)
W = 29.3           # overall width (Y)
HB = 10.4          # base plate thickness
H = 20.85          # overall height (top of boss)
BL = 33.2          # boss length along X (boss spans the full width)

R_EDGE = 3.0       # fillet on all upper edges (convex and concave)
C_BOT = 0.3        # small chamfer on the bottom edges

# counterbored mounting holes in the base (vertical)
HOLE_X = 33.2      # +/- X position of the holes
CB_D = 10.5        # counterbore diameter
CB_DEPTH = 4.4     # counterbore depth (to the start of the drill-point floor)
THRU_D = 6.5       # clearance hole diameter
POINT_ANGLE = 118.0  # drill-point angle of the counterbore floors

# rectangular window through boss and base (vertical)
WIN_X = 20.0
WIN_Y = 16.2
WIN_R = 3.0        # corner radius of the window
RELIEF_Z = 5.7     # height of the relief step inside the window (from the bottom face)
RELIEF_W = 0.3     # the lower section of the window is this much larger per side

# cross hole through the boss (along Y), counterbored from both sides
XH_Z = 9.7
XCB_D = 10.5
XCB_DEPTH = 4.5
XTHRU_D = 6.5

VIEW = {"azimuth": 45, "elevation": 26}


def cbore_cutter(d_thru, d_cb, depth_cb, length):
    """Counterbore tool: axis +Z, entry face at z=0, reaching down to z=-length.
    The counterbore floor is a drill-point cone running down into the through hole."""
    r1, r2 = d_thru / 2.0, d_cb / 2.0
    cone_h = (r2 - r1) / math.tan(math.radians(POINT_ANGLE / 2.0))
    pts = [
        (0, -length), (r1, -length), (r1, -depth_cb - cone_h),
        (r2, -depth_cb), (r2, 5.0), (0, 5.0),
    ]
    # sketch in the XZ plane (local x = radius, local y = global Z) and revolve about Z
    return cq.Workplane("XZ").polyline(pts).close().revolve(360, (0, 0, 0), (0, 1, 0))


def window_prism(wx, wy, r, z0, z1):
    """Rounded-rectangle prism centred on the Z axis, from z0 to z1."""
    return (cq.Workplane("XY").workplane(offset=z0)
            .sketch().rect(wx, wy).vertices().fillet(r).finalize()
            .extrude(z1 - z0))


# ---------------- body: stepped side profile extruded along Y ----------------
profile = [
    (-L / 2, 0), (L / 2, 0), (L / 2, HB), (BL / 2, HB),
    (BL / 2, H), (-BL / 2, H), (-BL / 2, HB), (-L / 2, HB),
]
body = (
    cq.Workplane("XZ")
    .polyline(profile).close()
    .extrude(W / 2, both=True)
)

# fillet every edge except those of the bottom face, then chamfer the bottom edges
body = body.edges("not <Z").fillet(R_EDGE)
body = body.faces("<Z").edges().chamfer(C_BOT)

# ---------------- holes and cut-outs ----------------
# vertical counterbored mounting holes in the base
for sx in (-1, 1):
    tool = cbore_cutter(THRU_D, CB_D, CB_DEPTH, HB + 2).translate((sx * HOLE_X, 0, HB))
    body = body.cut(tool)

# rectangular window through boss and base; its lowest section is relieved slightly
body = body.cut(window_prism(WIN_X, WIN_Y, WIN_R, RELIEF_Z - 0.5, H + 1))
body = body.cut(window_prism(WIN_X + 2 * RELIEF_W, WIN_Y + 2 * RELIEF_W, WIN_R + RELIEF_W,
                             -1, RELIEF_Z))

# cross hole along Y, counterbored from both side faces of the boss
for sy in (-1, 1):
    tool = cbore_cutter(XTHRU_D, XCB_D, XCB_DEPTH, W / 2 + 1)
    # turn the tool so its axis points out of the side face it enters from
    tool = tool.rotate((0, 0, 0), (1, 0, 0), 90 if sy < 0 else -90)
    tool = tool.translate((0, sy * W / 2, XH_Z))
    body = body.cut(tool)

result = body
